import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
T = 2.5                 # plate thickness

# plate outline (nearly symmetric about X = 0); Y runs along the length
Y_TOP = 50.0            # +Y end (apex of shallow end arc)
Y_BOT = -50.0           # -Y end (apex of rounded nose)
W_HALF = 31.05          # half width of the wide middle section
W_NECK = 24.5           # half width of the narrow +Y section
Y_WIDE_TOP_R = 23.0     # +X side: where the wide section starts tapering toward +Y
Y_WIDE_TOP_L = 19.6     # -X side: the taper starts lower (outline is not symmetric here)
Y_NECK_BOT = 37.6       # start of the narrow straight section
R_CORNER = 8.0          # corner radius at the +Y end (tangent to side and end arc)
END_R = 120.0           # radius of the shallow +Y end arc
Y_WIDE_BOT = -27.2      # where the wide section starts curving into the nose
NOSE_B = (15.0, -46.4)  # where the straight nose chamfers meet the nose arc

# elliptical cone boss
CONE_Y = -28.1
CONE_BASE = (16.0, 10.5)   # semi axes at plate top (X, Y)
CONE_TOP = (12.0, 7.35)     # semi axes at top of steep flank
CONE_H = 12.4               # height of steep flank
CHAMF_TOP = (9.75, 5.25)      # semi axes of the flat top face
CHAMF_H = 1.65              # height of the top chamfer band

# tube on top of the cone
TUBE_D = 8.8
TUBE_H = 5.4
TUBE_HOLE_D = 6.1
TUBE_HOLE_DEPTH = 5.0

# pins
PIN_D = 8.8
PIN_H = 25.5
PIN_YS = [19.3, 34.1]

# through holes
HOLE_D = 9.6
HOLE_YS = [7.7, -14.4]

# angle (deg) at which closed curves start, so their seams sit on the
# silhouette of the usual three-quarter views
SEAM_DEG = 45.0


# ---------------- helpers ----------------
def ellipse_wire(a, b, x, y, z):
    """closed ellipse wire; start point where the normal points along (1,1)"""
    t0 = math.degrees(math.atan2(b, a))
    e = cq.Edge.makeEllipse(a, b, cq.Vector(x, y, z), cq.Vector(0, 0, 1),
                            cq.Vector(1, 0, 0), t0, t0 + 360.0)
    return cq.Wire.assembleEdges([e])


def circle_wire(r, x, y, z):
    e = cq.Edge.makeCircle(r, cq.Vector(x, y, z), cq.Vector(0, 0, 1),
                           SEAM_DEG, SEAM_DEG + 360.0)
    return cq.Wire.assembleEdges([e])


def cylinder(r, x, y, z, h):
    f = cq.Face.makeFromWires(circle_wire(r, x, y, z))
    return cq.Solid.extrudeLinear(f, cq.Vector(0, 0, h))


def frustum(ab0, ab1, x, y, z0, h):
    w0 = ellipse_wire(ab0[0], ab0[1], x, y, z0)
    w1 = ellipse_wire(ab1[0], ab1[1], x, y, z0 + h)
    return cq.Solid.makeLoft([w0, w1], True)


# ---------------- plate ----------------
A = (-W_HALF, Y_WIDE_BOT)          # start of the -X nose chamfer line
B = (-NOSE_B[0], NOSE_B[1])        # end of the chamfer line / start of nose arc
D = (0.0, Y_BOT)                   # apex of the nose arc

# +Y end: shallow arc (radius END_R, apex at Y_TOP) blended into the narrow
# straight sides by corner arcs of radius R_CORNER, tangent to both
ecy = Y_TOP - END_R                            # end-arc centre y
ccx = W_NECK - R_CORNER                        # corner-arc centre x
ccy = ecy + math.sqrt((END_R - R_CORNER) ** 2 - ccx ** 2)   # corner-arc centre y
ux, uy = ccx / (END_R - R_CORNER), (ccy - ecy) / (END_R - R_CORNER)
tp = (END_R * ux, ecy + END_R * uy)            # tangent point corner arc / end arc
mid_a = math.atan2(tp[1] - ccy, tp[0] - ccx) / 2.0   # half-way angle of corner arc
cm = (ccx + R_CORNER * math.cos(mid_a), ccy + R_CORNER * math.sin(mid_a))

outline = (
    cq.Workplane("XY")
    .moveTo(W_HALF, Y_WIDE_BOT)
    .lineTo(W_HALF, Y_WIDE_TOP_R)
    .lineTo(W_NECK, Y_NECK_BOT)
    .lineTo(W_NECK, ccy)
    .threePointArc(cm, tp)
    .threePointArc((0, Y_TOP), (-tp[0], tp[1]))
    .threePointArc((-cm[0], cm[1]), (-W_NECK, ccy))
    .lineTo(-W_NECK, Y_NECK_BOT)
    .lineTo(-W_HALF, Y_WIDE_TOP_L)
    .lineTo(A[0], A[1])
    .lineTo(B[0], B[1])
    .threePointArc(D, (-B[0], B[1]))      # rounded nose
    .close()                              # straight chamfer line back to the start
)
plate = outline.extrude(T)

# through holes in the plate only (the cone boss partly roofs the one next to it)
for hy in HOLE_YS:
    plate = plate.cut(cq.Workplane().add(cylinder(HOLE_D / 2.0, 0.0, hy, -1.0, T + 2.0)))

# ---------------- elliptical cone boss ----------------
cone = frustum(CONE_BASE, CONE_TOP, 0.0, CONE_Y, T, CONE_H)
chamf = frustum(CONE_TOP, CHAMF_TOP, 0.0, CONE_Y, T + CONE_H, CHAMF_H)
z_flat = T + CONE_H + CHAMF_H

tube = cylinder(TUBE_D / 2.0, 0.0, CONE_Y, z_flat, TUBE_H)

# ---------------- pins ----------------
body = plate.union(cq.Workplane().add(cone)).union(cq.Workplane().add(chamf))
body = body.union(cq.Workplane().add(tube))
for py in PIN_YS:
    body = body.union(cq.Workplane().add(cylinder(PIN_D / 2.0, 0.0, py, T, PIN_H)))

# ---------------- blind bore in the tube ----------------
body = body.cut(
    cq.Workplane().add(
        cylinder(TUBE_HOLE_D / 2.0, 0.0, CONE_Y,
                 z_flat + TUBE_H - TUBE_HOLE_DEPTH, TUBE_HOLE_DEPTH + 1.0)
    )
)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
